import math
import cadquery as cq

# =====================================================================
# Coil-over shock absorber: lower eye, conical lower mount, damper tube,
# wider damper body, two perforated spring seats, flat-band (tapered
# section) left-hand coil spring, ogive top mount and upper eye.
# Z is the shock axis, eyes have their bores along Y.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
# lower eye
BOT_EYE_Z = 10.4          # centre height of lower eye
BOT_EYE_OD = 20.0
BOT_EYE_ID = 14.0
BOT_EYE_T = 9.5           # thickness along Y

# lower mount (ogive taper from the tube down to the lower eye)
LM_TOP_Z = 33.1           # junction with the damper tube
LM_MID = (7.65, 26.45)    # (r, z) point on the taper
LM_LOW = (4.3, 20.7)      # (r, z) point on the taper near the eye
LM_END_Z = 18.6           # taper is buried in the eye ring below this

# damper tube and body
TUBE_D = 20.0
STEP_Z = 106.3            # where the wider damper body starts
BODY_D = 28.8

# spring seats (flanges)
FL_D = 50.8
FL_T = 5.4
BFL_Z1 = 87.3             # bottom seat upper face
TFL_Z0 = 182.5            # top seat lower face
HOLE_D = 8.4
HOLE_PCD_R = 17.4
N_HOLES = 4

# top ogive mount
NOSE_LIFT = 0.5           # small neck between seat and ogive base
NOSE_R0 = 14.95
NOSE_P1 = (11.25, 10.0)   # (r, dz above ogive base)
NOSE_P2 = (6.75, 20.0)
NOSE_POKE = 0.3           # domed tip pokes this far into the eye bore
NOSE_DOME_H = 0.85        # height of the shallow dome closing the ogive

# upper eye
TOP_EYE_Z = 222.3
TOP_EYE_OD = 30.3
TOP_EYE_ID = 20.5
TOP_EYE_T = 11.4
EYE_FILLET = 1.2
BOT_EYE_FILLET = 0.8

# coil spring: flat band helix, left handed, whole number of turns
SPR_TURNS = 6
SPR_RI = BODY_D / 2 - 0.3
SPR_RO = FL_D / 2 - 0.05
SPR_T_IN = 5.0           # band thickness at the inner (body) edge
SPR_T_OUT = 1.0          # band thickness at the outer rim (tapered section)
SPR_EMBED = 0.9           # band centre line runs this far into each seat

BFL_Z0 = BFL_Z1 - FL_T
TFL_Z1 = TFL_Z0 + FL_T
SEAM_ROT = 90.0           # put surface seams on the +Y side


def circle3(p1, p2, p3):
    """Centre and radius of the circle through three 2D points."""
    (x1, y1), (x2, y2), (x3, y3) = p1, p2, p3
    d = 2 * (x1 * (y2 - y3) + x2 * (y3 - y1) + x3 * (y1 - y2))
    s1, s2, s3 = x1 ** 2 + y1 ** 2, x2 ** 2 + y2 ** 2, x3 ** 2 + y3 ** 2
    ux = (s1 * (y2 - y3) + s2 * (y3 - y1) + s3 * (y1 - y2)) / d
    uy = (s1 * (x3 - x2) + s2 * (x1 - x3) + s3 * (x2 - x1)) / d
    return ux, uy, math.hypot(x1 - ux, y1 - uy)


def arc_r(c, z):
    cx, cz, cr = c
    return cx + math.sqrt(cr ** 2 - (z - cz) ** 2)


def revolve_arc_solid(z_a, r_a, z_b, c):
    """Solid of revolution bounded by the axis, two flat ends and an arc
    (circle c) running from z_a (radius r_a) to z_b."""
    z_m = 0.5 * (z_a + z_b)
    r_b = arc_r(c, z_b)
    s = (cq.Workplane("XZ")
         .moveTo(0, z_a)
         .lineTo(r_a, z_a)
         .threePointArc((arc_r(c, z_m), z_m), (r_b, z_b))
         .lineTo(0, z_b)
         .close()
         .revolve(360, (0, 0, 0), (0, 1, 0)))
    return s.rotate((0, 0, 0), (0, 0, 1), SEAM_ROT)


def cyl(r, z0, z1):
    c = cq.Workplane("XY").workplane(offset=z0).circle(r).extrude(z1 - z0)
    return c.rotate((0, 0, 0), (0, 0, 1), SEAM_ROT)


# ---------------- axial parts ----------------
tube = cyl(TUBE_D / 2, LM_TOP_Z - 0.01, STEP_Z + 0.01)
body = cyl(BODY_D / 2, STEP_Z, TFL_Z1 + NOSE_LIFT + 0.01)

# lower mount taper
lm_c = circle3((TUBE_D / 2, LM_TOP_Z), LM_MID, LM_LOW)
lower_mount = revolve_arc_solid(LM_TOP_Z, TUBE_D / 2, LM_END_Z, lm_c)


def seat(z0):
    f = cq.Workplane("XY").workplane(offset=z0).circle(FL_D / 2).extrude(FL_T)
    f = f.rotate((0, 0, 0), (0, 0, 1), SEAM_ROT)
    holes = (cq.Workplane("XY").workplane(offset=z0 - 1)
             .polarArray(HOLE_PCD_R, 0, 360, N_HOLES)
             .circle(HOLE_D / 2).extrude(FL_T + 2))
    return f.cut(holes)


bseat = seat(BFL_Z0)
tseat = seat(TFL_Z0)

# top ogive mount
nz0 = TFL_Z1 + NOSE_LIFT
nose_c = circle3((NOSE_R0, nz0),
                 (NOSE_P1[0], nz0 + NOSE_P1[1]),
                 (NOSE_P2[0], nz0 + NOSE_P2[1]))
nose_top = TOP_EYE_Z - TOP_EYE_ID / 2 + NOSE_POKE
nose_ze = nose_top - NOSE_DOME_H                # end of the ogive flank
nose_re = arc_r(nose_c, nose_ze)
nose_zm = 0.5 * (nz0 + nose_ze)
dome_R = (nose_re ** 2 + NOSE_DOME_H ** 2) / (2 * NOSE_DOME_H)
dome_a = math.atan2(nose_re, dome_R - NOSE_DOME_H) / 2
nose = (cq.Workplane("XZ")
        .moveTo(0, nz0)
        .lineTo(NOSE_R0, nz0)
        .threePointArc((arc_r(nose_c, nose_zm), nose_zm), (nose_re, nose_ze))
        .threePointArc((dome_R * math.sin(dome_a),
                        nose_top - dome_R + dome_R * math.cos(dome_a)),
                       (0, nose_top))
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), SEAM_ROT))


# ---------------- eyes ----------------
def eye(zc, od, idd, t, fr):
    e = (cq.Workplane("XZ").workplane(offset=-t / 2).center(0, zc)
         .circle(od / 2).extrude(t))
    e = e.edges("%CIRCLE").fillet(fr)
    bore = (cq.Workplane("XZ").workplane(offset=-t).center(0, zc)
            .circle(idd / 2).extrude(2 * t))
    return e.cut(bore)


top_eye = eye(TOP_EYE_Z, TOP_EYE_OD, TOP_EYE_ID, TOP_EYE_T, EYE_FILLET)
bot_eye = eye(BOT_EYE_Z, BOT_EYE_OD, BOT_EYE_ID, BOT_EYE_T, BOT_EYE_FILLET)

# ---------------- spring ----------------
z_lo = BFL_Z1 - SPR_EMBED                  # band centre at lower end
z_hi = TFL_Z0 + SPR_EMBED                  # band centre at upper end
H = z_hi - z_lo
pitch = H / SPR_TURNS
r_mid_spr = 0.5 * (SPR_RI + SPR_RO)
helix = cq.Wire.makeHelix(pitch, H, r_mid_spr, lefthand=True)
prof = (cq.Workplane("XZ")
        .polyline([(SPR_RI, -SPR_T_IN / 2), (SPR_RO, -SPR_T_OUT / 2),
                   (SPR_RO, SPR_T_OUT / 2), (SPR_RI, SPR_T_IN / 2)])
        .close())
spring = prof.sweep(cq.Workplane().add(helix), isFrenet=True)
spring = spring.translate((0, 0, z_lo))    # both ends lie on +X

# the seats are drilled before the spring is fitted, so the band ends
# partly fill the holes right above/below them
result = (tube.union(body).union(lower_mount).union(bseat).union(tseat)
          .union(nose).union(top_eye).union(bot_eye).union(spring))

VIEW = {"azimuth": 45, "elevation": 26}
